import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
D_BASE = 40.0          # diameter of the flat back (+Y) face
L = 19.2               # overall axial length (along Y)
ARC_R = 33.0           # radius of the dome profile arc (tangent to the axis direction at the base)
FRONT_FILLET = 1.0     # round on the front face outer edge
HEX_AF = 15.4          # hex pocket across flats
BACK_WALL = 3.0        # thickness left behind the hex pocket
HEX_DEPTH = L - BACK_WALL  # hex pocket depth from the front face
HEX_FILLET = 0.55      # round on the hex pocket opening edges
HOLE_D = 8.3           # through hole diameter (back wall)
SEAM_ANGLE = 165.0     # where the revolve seam is parked (cosmetic only)

R = D_BASE / 2.0

# ---------------- dome body (revolved about Y) ----------------
# profile in (r, y): front face at y = 0, flat base at y = L
def r_at(a):
    """radius of the dome at axial distance a from the base"""
    return R - ARC_R + math.sqrt(ARC_R ** 2 - a ** 2)

r_front = r_at(L)
a_mid = L / 2.0
prof = (
    cq.Workplane("XY")
    .moveTo(0, 0)
    .lineTo(r_front, 0)
    .threePointArc((r_at(a_mid), L - a_mid), (R, L))
    .lineTo(0, L)
    .close()
)
body = prof.revolve(360, (0, 0, 0), (0, 1, 0))
body = body.rotate((0, 0, 0), (0, 1, 0), SEAM_ANGLE)

# round the front face outer edge
body = body.faces("<Y").edges().fillet(FRONT_FILLET)

# ---------------- hex pocket in the front (-Y) face ----------------
hex_ac = HEX_AF / math.cos(math.radians(30))   # across corners
# "XZ" workplane: normal is -Y, so a negative extrude goes toward +Y (into the part)
pocket = cq.Workplane("XZ").polygon(6, hex_ac).extrude(-HEX_DEPTH)
# rotate so the corners point along +/-Z (flats perpendicular to X)
pocket = pocket.rotate((0, 0, 0), (0, 1, 0), 90)
body = body.cut(pocket)

# round the hex opening edges (edges lying in the front face plane y = 0)
hex_rim = cq.selectors.AndSelector(
    cq.selectors.BoxSelector((-hex_ac, -0.01, -hex_ac), (hex_ac, 0.01, hex_ac)),
    cq.selectors.TypeSelector("LINE"),
)
body = body.edges(hex_rim).fillet(HEX_FILLET)

# ---------------- through hole in the back wall ----------------
hole = cq.Workplane("XZ").circle(HOLE_D / 2.0).extrude(-L * 2).translate((0, -L / 2, 0))
body = body.cut(hole)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
